"""Square enclosure frame / bezel ring.

Open rounded-square ring: thin side walls, an inward bottom flange with a
square opening, a narrow bottom lip with round corner feet, a vertical
screw/light-pipe channel in every inner corner, shallow corner pockets in the
top rim, a round hole in the front wall and a cable notch in the lip.
"""
import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # outer square size
H = 36.0           # overall height
RO = 8.8           # outer corner radius
T = 3.2            # wall thickness
F = 3.1            # bottom flange inward extent (beyond wall inner face)
HL = 3.75          # bottom lip / flange height
EW = 2.8           # lip inset from the outer wall face (along the walls)
RF = 7.15          # corner foot radius (concentric with the outer corner arc)
RFJ = 1.5          # blend radius foot / lip
RC = 6.9           # corner channel radius (concentric with the outer corner arc)
RJ = 1.0           # vertical blend radius channel / wall
FIL_IN = 2.95      # fillet wall / flange junction
RIM = 1.2          # remaining outer rim thickness at the top corner pockets
PD = 3.05          # corner pocket depth
LA = 20.2          # pocket length along the +/-Y walls (measured from X faces)
LB = 14.7          # pocket length along the +/-X walls (measured from Y faces)
HOLE_D = 12.0      # side hole diameter (front, -Y face)
HOLE_X = -23.5     # side hole x position
HOLE_Z = 14.6      # side hole centre height
NOTCH_R = 7.45     # notch radius in the lip (+X face)
NOTCH_Y = 27.6     # notch centre y
NOTCH_ZC = HL - 0.15 - NOTCH_R   # notch axis height (arc top just under the flange top)

C = W / 2 - RO     # corner arc centre offset (shared by channel, foot, lobe)


def corner_locs(off):
    """Locations at the four corners; local x axis points to the part centre
    so circle seams end up on the side that gets removed."""
    locs = []
    for sx in (-1, 1):
        for sy in (-1, 1):
            ang = math.degrees(math.atan2(-sy, -sx))
            locs.append(cq.Location(cq.Vector(sx * off, sy * off, 0),
                                    cq.Vector(0, 0, 1), ang))
    return locs


def prism(sketch, z0, h):
    """Extrude a sketch from z0 by h."""
    return cq.Workplane("XY").workplane(offset=z0).placeSketch(sketch).extrude(h)


# ---------------- upper wall ----------------
outer = prism(cq.Sketch().rect(W, W).vertices().fillet(RO), HL, H - HL)

# cavity: square with round corners, plus the corner channels (small blends)
cav_sk = (cq.Sketch().rect(W - 2 * T, W - 2 * T).vertices().fillet(RO - T)
          .reset().push(corner_locs(C)).circle(RC).clean()
          .reset().vertices().fillet(RJ))
cavity = prism(cav_sk, HL, H - HL)
wall = outer.cut(cavity)

# ---------------- bottom lip / flange ring ----------------
lip_sk = (cq.Sketch().rect(W - 2 * EW, W - 2 * EW).vertices().fillet(RO - EW)
          .reset().push(corner_locs(C)).circle(RF).clean()
          .reset().vertices().fillet(RFJ))
ring_outer = prism(lip_sk, 0.0, HL)
# flange opening = cavity eroded by F (lobes at the corners, rounded junctions)
open_sk = (cq.Sketch().rect(W - 2 * (T + F), W - 2 * (T + F))
           .push(corner_locs(C)).circle(RC - F).clean()
           .reset().vertices().fillet(F + RJ))
ring = ring_outer.cut(prism(open_sk, -1.0, HL + 2.0))

body = wall.union(ring)

# ---------------- fillet wall inner face / channel to flange top ----------------
cav_wire = cavity.faces("<Z").val().outerWire()


def _inner_junction(e):
    bb = e.BoundingBox()
    if abs(bb.zmin - HL) > 1e-4 or abs(bb.zmax - HL) > 1e-4:
        return False
    mid = cq.Vertex.makeVertex(*e.positionAt(0.5).toTuple())
    return cav_wire.distance(mid) < 1e-4


body = body.newObject([e for e in body.edges().vals() if _inner_junction(e)]).fillet(FIL_IN)

# ---------------- corner pockets in the top rim ----------------
rim_in = prism(cq.Sketch().rect(W - 2 * RIM, W - 2 * RIM).vertices().fillet(RO - RIM),
               H - PD, PD + 1.0)
boxes = None
for sx in (-1, 1):
    for sy in (-1, 1):
        x0 = W / 2 - LA if sx > 0 else -W / 2
        y0 = W / 2 - LB if sy > 0 else -W / 2
        b = (cq.Workplane("XY").box(LA, LB, PD + 1.0, centered=False)
             .translate((x0, y0, H - PD)))
        boxes = b if boxes is None else boxes.union(b)
body = body.cut(rim_in.intersect(boxes))

# ---------------- round hole in the front (-Y) wall ----------------
hole = (cq.Workplane("XZ").center(HOLE_X, HOLE_Z).circle(HOLE_D / 2)
        .extrude(-4 * T).translate((0, -W / 2 - T, 0)))
body = body.cut(hole)

# ---------------- cable notch through the lip on the +X side ----------------
notch = (cq.Workplane("YZ").center(NOTCH_Y, NOTCH_ZC).circle(NOTCH_R)
         .extrude(T + F + 2).translate((W / 2 - T - F - 1, 0, 0)))
notch = notch.intersect(cq.Workplane("XY").box(W, W, HL + 1, centered=(True, True, False))
                        .translate((0, 0, -1)))
body = body.cut(notch)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
